import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Robotic hand palm: wrist cup (base), palm shell, three finger knuckles,
# thumb notch with roller, electronics box and brackets on the -X side.
# X = thickness (back of hand +X), Y = width (finger row), Z = up.
# ---------------------------------------------------------------------------

# ---- wrist base ----
BASE_CY = 2.5          # base axis Y offset
BASE_R = 24.75         # radius at the bottom (slight draft upwards)
BASE_H = 18.0
BASE_TAPER = 3.0
BORE_R = 19.3
BORE_D = 12.0
RH_Z = 5.8             # radial hole height
RH_D = 3.6             # radial hole dia
RH_CB = 6.2            # counterbore dia
N_RH = 8

# ---- palm shell ----
X_IN = 3.5             # -X face of shell
X_OUT = 24.5           # +X face (max)
WALL = 3.5             # rim / wall thickness
SHELL_R = 10.0         # rounding of the +X face boundary
RIM_C = 5.5            # bevel band height on the rim's outer top edge
RIM_TAPER = 22.0       # bevel angle from vertical
DECK_Z = 88.0          # deck under the knuckles

# rim heights (from -Y end to +Y end)
RIM1, RIM2, RIM3, RIM4 = 91.3, 93.5, 96.4, 93.7
END_NEG_Z = 97.4
END_POS_Z = 102.0

# ---- knuckles ----
K_Y = [-32.4, -12.2, 8.0]
K_AXZ = [103.0, 106.5, 109.5]
K_X = 6.5
K_R = 9.5
K_W = 11.5
HUB_R = 6.6

# ---- box ----
BOX_X0, BOX_X1 = -14.25, X_IN
BOX_Y0, BOX_Y1 = -26.4, 13.0
BOX_Z0, BOX_Z1 = 40.5, 88.5

# ---- thumb notch ----
TN_Y0 = 14.0
TN_Z0, TN_Z1 = 21.5, 40.0
TR_Y, TR_X, TR_R = 26.5, 13.0, 9.0
MNT_X1 = 22.5          # +X face of the thumb roller mount
CAV_X1 = 12.7          # back of the thumb-side cavity
RAMP_X0 = -8.9         # -X side plate next to knuckle 3
LIP_X0 = -1.5          # the thumb lip reaches slightly past the -X face


def yz_profile():
    """Side silhouette of the shell (Y,Z), extruded through X."""
    left = [(-47.3, 82.0), (-47.5, 68.0), (-46.4, 56.0), (-44.4, 47.0),
            (-41.5, 39.1), (-37.7, 31.4), (-32.3, 24.5), (-25.6, 19.2),
            (-19.0, 16.0)]
    w = (cq.Workplane("YZ", origin=(X_IN, 0, 0))
         .moveTo(-19.0, 16.0)
         .lineTo(27.0, 16.0)
         .spline([(40.0, 24.0), (46.5, 40.0)], includeCurrent=True)
         .spline([(47.0, 70.0), (46.0, 90.0), (43.5, END_POS_Z)], includeCurrent=True)
         .lineTo(40.0, END_POS_Z)
         .lineTo(40.0, RIM4)
         .lineTo(15.0, RIM4)
         .lineTo(13.5, RIM3)
         .lineTo(-0.7, RIM3)
         .lineTo(-3.0, RIM2)
         .lineTo(-20.5, RIM2)
         .lineTo(-23.1, RIM1)
         .lineTo(-39.0, RIM1)
         .threePointArc((-41.4, 95.3), (-43.0, END_NEG_Z))
         .lineTo(-46.0, END_NEG_Z)
         .spline(left[:-1], includeCurrent=True)
         .close())
    return w.extrude(X_OUT + 2 - X_IN)


def xy_profile():
    """Top-view outline: slightly convex +X face."""
    w = (cq.Workplane("XY", origin=(0, 0, 0))
         .moveTo(X_IN - 1, -60.0)
         .lineTo(X_OUT - 3.3, -60.0)
         .threePointArc((X_OUT, 0.0), (X_OUT - 3.3, 60.0))
         .lineTo(X_IN - 1, 60.0)
         .close())
    return w.extrude(130)


def outline_sketch(y0, y1, r):
    """Top-view outline of the shell with its +X corners rounded (for the rim bevel)."""
    big = (60.0 ** 2 + 3.3 ** 2) / (2 * 3.3)

    def xa(y):
        return X_OUT - big + math.sqrt(big * big - y * y)

    return (cq.Sketch()
            .segment((X_IN - 1, y0), (xa(y0), y0))
            .arc((xa(y0), y0), (X_OUT, 0.0), (xa(y1), y1))
            .segment((X_IN - 1, y1))
            .close()
            .assemble()
            .vertices("not <X")
            .fillet(r))


def build_shell():
    body = yz_profile().intersect(xy_profile())
    # round the +X face boundary (sides and bottom)
    fx = body.faces(">X").edges().vals()
    big = [e for e in fx if e.BoundingBox().zmin < 45]
    body = body.newObject(big).fillet(SHELL_R)
    # bevel band along the rim's outer top edge (follows the rim steps)
    for (zr, ya, yb) in [(95.6, -42.6, -41.8), (94.2, -41.8, -40.9), (92.6, -40.9, -39.8),
                         (RIM1, -39.8, -20.5), (RIM2, -23.1, -0.7),
                         (RIM3, -3.0, 14.0), (RIM4, 14.0, 40.0)]:
        taper = (cq.Workplane("XY", origin=(0, 0, zr - RIM_C))
                 .placeSketch(outline_sketch(-47.3, 46.5, SHELL_R))
                 .extrude(12.0, taper=RIM_TAPER))
        slab = (cq.Workplane("XY").box(16.0, yb - ya, 12.0, centered=False)
                .translate((14.0, ya, zr - RIM_C)))
        body = body.cut(slab.cut(taper))

    # -Y end wall top rounding (circle about Y axis, centre (X=3, Z=75), R=22)
    cut_neg = (cq.Workplane("XY").box(40, 20, 40, centered=False)
               .translate((3.0, -60.0, 75.0)))
    cyl = (cq.Workplane("XZ", origin=(0, -40, 0)).center(3.0, 75.0)
           .circle(22.0).extrude(25))
    body = body.cut(cut_neg.cut(cyl))

    # +Y end wall top rounding (circle about Y axis, centre (X=5.75, Z=84.15), R=17.85)
    cut_pos = (cq.Workplane("XY").box(30, 20, 40, centered=False)
               .translate((5.75, 39.0, 84.15)))
    cyl2 = (cq.Workplane("XZ", origin=(0, 60, 0)).center(5.75, 84.15)
            .circle(17.85).extrude(25))
    body = body.cut(cut_pos.cut(cyl2))

    # top pocket inside the rim (deck below the knuckles)
    top_pocket = (cq.Workplane("XY")
                  .box(X_OUT - WALL - X_IN + 5, 40.0 + 43.0, 60, centered=False)
                  .translate((X_IN - 5, -43.0, DECK_Z)))
    body = body.cut(top_pocket)

    # thumb-side cavity open to -X and top
    cav = (cq.Workplane("XY")
           .box(CAV_X1 - X_IN + 5, 40.5 - 16.0, 80, centered=False)
           .translate((X_IN - 5, 16.0, 42.0)))
    body = body.cut(cav)
    # inner shelf in the cavity
    shelf = (cq.Workplane("XY").box(CAV_X1 - X_IN + 0.5, 9.0, 12.0, centered=False)
             .translate((X_IN - 0.5, 16.0, 42.0)))
    body = body.union(shelf)
    # thick +X wall portion beside the thumb-side cavity
    fill = (cq.Workplane("XY")
            .box(X_OUT - WALL - CAV_X1 + 0.3, 40.6 - 16.8, RIM4 - 0.6 - (DECK_Z - 1), centered=False)
            .translate((CAV_X1, 16.8, DECK_Z - 1)))
    body = body.union(fill)

    # thumb notch (through in X), slanted inner edge
    notch = (cq.Workplane("YZ", origin=(-10, 0, 0))
             .polyline([(TN_Y0 + 2.0, TN_Z0), (60.0, TN_Z0), (60.0, TN_Z1),
                        (TN_Y0, TN_Z1)]).close().extrude(50))
    body = body.cut(notch)

    # lip under the thumb notch
    lip = (cq.Workplane("YZ", origin=(LIP_X0, 0, 0))
           .polyline([(TN_Y0, 16.0), (27.0, 16.0), (37.0, TN_Z0), (TN_Y0, TN_Z0)])
           .close().extrude(X_OUT - 2.5 - LIP_X0))
    try:
        lip = lip.edges("|Z").edges("<X").fillet(3.0)
    except Exception:
        pass
    lslot = (cq.Workplane("XY", origin=(0, 0, 15.0)).center(LIP_X0 + 3.5, 25.0)
             .slot2D(12.0, 2.0, angle=90).extrude(8.0))
    lip = lip.cut(lslot)
    try:
        lip = lip.faces(">X").edges().fillet(2.0)
    except Exception:
        pass
    body = body.union(lip)
    return body


def build_base():
    r_top = BASE_R - BASE_H * math.tan(math.radians(BASE_TAPER))
    base = (cq.Workplane("XZ")
            .polyline([(0, 0), (BASE_R - 0.8, 0), (BASE_R, 0.8), (r_top, BASE_H), (0, BASE_H)])
            .close()
            .revolve(360, (0, 0, 0), (0, 1, 0)))
    base = base.faces(">Z").edges().fillet(2.5)
    base = base.translate((0, BASE_CY, 0))
    bore = cq.Workplane("XY").center(0, BASE_CY).circle(BORE_R - 1.0).extrude(BORE_D)
    step = cq.Workplane("XY").center(0, BASE_CY).circle(BORE_R).extrude(2.5)
    base = base.cut(bore).cut(step)
    # radial counterbored holes
    for i in range(N_RH):
        a = i * 360.0 / N_RH
        hole = (cq.Workplane("YZ").center(0, RH_Z).circle(RH_D / 2).extrude(BASE_R + 2))
        cb = (cq.Workplane("YZ", origin=(BASE_R - 1.0, 0, 0)).center(0, RH_Z)
              .circle(RH_CB / 2).extrude(3))
        h = hole.union(cb).rotate((0, 0, 0), (0, 0, 1), a).translate((0, BASE_CY, 0))
        base = base.cut(h)
    # holes in the bore ceiling
    for (hx, hy) in [(0.0, 0.0), (8.0, 8.0), (-8.0, 8.0), (8.0, -8.0), (-8.0, -8.0)]:
        ch = (cq.Workplane("XY", origin=(0, 0, BORE_D - 0.01)).center(hx, hy + BASE_CY)
              .circle(1.6).extrude(4))
        cb = (cq.Workplane("XY", origin=(0, 0, BORE_D - 0.01)).center(hx, hy + BASE_CY)
              .circle(2.8).extrude(1.2))
        base = base.cut(ch).cut(cb)
    return base


def build_knuckle(yc, axz):
    ped_top = axz - 6.0
    px1 = K_X + K_R                      # pedestal flush with the knuckle's +X face
    ped = (cq.Workplane("XY")
           .box(px1 + 4.0, (yc + 8.4) - (yc - K_W / 2), ped_top - (DECK_Z - 1), centered=False)
           .translate((-4.0, yc - K_W / 2, DECK_Z - 1)))
    ledge = (cq.Workplane("XY")
             .box(px1 + 4.0, 9.6 - K_W / 2 + 0.01, ped_top - 2.5 - (DECK_Z - 1), centered=False)
             .translate((-4.0, yc - 9.6, DECK_Z - 1)))
    ped = ped.union(ledge)
    # tombstone: rectangle + half-disc, axis along Y
    tomb = (cq.Workplane("XZ", origin=(0, yc + K_W / 2, 0))
            .moveTo(K_X - K_R, ped_top - 0.5)
            .lineTo(K_X + K_R, ped_top - 0.5)
            .lineTo(K_X + K_R, axz)
            .threePointArc((K_X, axz + K_R), (K_X - K_R, axz))
            .close()
            .extrude(K_W))
    # hub boss on -Y face
    hub = (cq.Workplane("XZ", origin=(0, yc - K_W / 2 + 0.01, 0)).center(K_X, axz)
           .circle(HUB_R).extrude(1.3))
    hub = hub.faces("<Y").edges().chamfer(1.0)
    # axle stub on +Y face
    stub = (cq.Workplane("XZ", origin=(0, yc + K_W / 2 + 1.5, 0)).center(K_X, axz)
            .circle(2.0).extrude(1.5))
    k = ped.union(tomb).union(hub).union(stub)
    # hub holes
    yface = yc - K_W / 2 - 1.3
    ch = (cq.Workplane("XZ", origin=(0, yface - 0.5, 0)).center(K_X, axz)
          .circle(1.8).extrude(-4.5))
    k = k.cut(ch)
    for i in range(4):
        a = math.radians(90 * i)
        sh = (cq.Workplane("XZ", origin=(0, yface - 0.5, 0))
              .center(K_X + 4.3 * math.cos(a), axz + 4.3 * math.sin(a))
              .circle(0.55).extrude(-2.5))
        k = k.cut(sh)
    # pedestal holes on +X face
    for dy in (-2.6, 2.6):
        ph = (cq.Workplane("YZ", origin=(px1 - 3.0, 0, 0)).center(yc + dy, ped_top - 2.3)
              .circle(0.8).extrude(3.5))
        pc = (cq.Workplane("YZ", origin=(px1 - 0.5, 0, 0)).center(yc + dy, ped_top - 2.3)
              .circle(1.4).extrude(1.0))
        k = k.cut(ph).cut(pc)
        qh = (cq.Workplane("YZ", origin=(-4.5, 0, 0)).center(yc + dy, ped_top - 2.3)
              .circle(0.8).extrude(3.0))
        k = k.cut(qh)
    return k


def build_box():
    box = (cq.Workplane("XY")
           .box(BOX_X1 - BOX_X0 + 0.5, BOX_Y1 - BOX_Y0, BOX_Z1 - BOX_Z0, centered=False)
           .translate((BOX_X0, BOX_Y0, BOX_Z0)))
    box = box.edges("|Y").edges("<X").fillet(0.8)
    # connector recess on the -Y face and a small vent slot
    rec = (cq.Workplane("XY").box(6.5, 3.0, 19.0, centered=False)
           .translate((-2.5, BOX_Y0 - 0.5, BOX_Z0 + 0.8)))
    box = box.cut(rec)
    vent = (cq.Workplane("XZ", origin=(0, BOX_Y0 + 1.0, 0)).center(-4.2, BOX_Z0 + 8.5)
            .slot2D(9.0, 1.2, angle=90).extrude(2.0))
    box = box.cut(vent)
    return box


def build_thumb_roller():
    # roller (axis Z) sitting in the thumb notch
    r = (cq.Workplane("XY", origin=(0, 0, 24.8)).center(TR_X, TR_Y)
         .circle(TR_R).extrude(11.2))
    r = r.edges().fillet(1.2)
    hub = (cq.Workplane("XY", origin=(0, 0, 35.0)).center(TR_X, TR_Y)
           .circle(6.2).extrude(TN_Z1 - 35.0))
    axle = (cq.Workplane("XY", origin=(0, 0, TN_Z0)).center(TR_X, TR_Y)
            .circle(3.0).extrude(TN_Z1 - TN_Z0))
    # mount block on the -Y side of the notch with two screws facing +X
    mount = (cq.Workplane("XY").box(MNT_X1 - X_IN, 19.0 - TN_Y0, TN_Z1 - TN_Z0, centered=False)
             .translate((X_IN, TN_Y0, TN_Z0)))
    for zz in (28.4, 33.4):
        h = (cq.Workplane("YZ", origin=(MNT_X1 - 3.0, 0, 0)).center(17.6, zz)
             .circle(0.7).extrude(3.5))
        c = (cq.Workplane("YZ", origin=(MNT_X1 - 0.6, 0, 0)).center(17.6, zz)
             .circle(1.2).extrude(1.0))
        mount = mount.cut(h).cut(c)
    return r.union(hub).union(axle).union(mount)


def build_brackets():
    # -Y end clip: thin frame standing off the -X side
    clip = (cq.Workplane("XZ", origin=(0, -40.8, 0)).center(-6.5, 92.0)
            .rect(7.0, 8.5).extrude(1.6))
    win = (cq.Workplane("XZ", origin=(0, -39.0, 0)).center(-7.0, 91.6)
           .rect(4.0, 5.5).extrude(5.0))
    clip = clip.cut(win)
    bar = (cq.Workplane("XY").box(4.0, 4.0, 1.6, centered=False)
           .translate((-6.0, -42.4, 94.6)))
    clip = clip.union(bar)
    # knuckle rail on -X side, joining the pedestals
    rail = (cq.Workplane("XY").box(3.0, 78.0, 6.0, centered=False)
            .translate((-6.5, -42.0, 86.0)))
    # sloped side plate on the -X side between knuckle 3 and the +Y end
    ramp = (cq.Workplane("YZ", origin=(RAMP_X0, 0, 0))
            .polyline([(12.0, 96.7), (12.0, 102.7), (19.6, 102.7), (34.8, 94.3),
                       (36.3, 94.3), (36.3, 88.5), (34.8, 88.5), (19.6, 96.7)])
            .close().extrude(2.5))
    rail = rail.union(ramp)
    # link plate (bent bar) on -X side, +Y of box
    pts = [(5.0, 97.0), (13.5, 90.5), (22.0, 83.5)]
    link = None
    for (a0, a1) in zip(pts[:-1], pts[1:]):
        ang = math.degrees(math.atan2(a1[1] - a0[1], a1[0] - a0[0]))
        length = math.hypot(a1[0] - a0[0], a1[1] - a0[1])
        seg = (cq.Workplane("YZ", origin=(-9.0, 0, 0))
               .center((a0[0] + a1[0]) / 2, (a0[1] + a1[1]) / 2)
               .transformed(rotate=(0, 0, ang))
               .slot2D(length + 6.5, 6.5)
               .extrude(2.0))
        link = seg if link is None else link.union(seg)
    for (yy, zz, rr) in [(5.0, 97.0, 1.2), (13.5, 90.5, 1.0), (22.0, 83.5, 2.0),
                         (9.0, 94.0, 0.7)]:
        hh = cq.Workplane("YZ", origin=(-10.0, 0, 0)).center(yy, zz).circle(rr).extrude(5)
        link = link.cut(hh)
    # stand-off posts tying the link to the shell
    for (yy, zz) in [(22.0, 83.5)]:
        post = (cq.Workplane("YZ", origin=(-7.0, 0, 0)).center(yy, zz)
                .rect(4.0, 4.0).extrude(CAV_X1 + 7.5))
        link = link.union(post)
    return clip.union(rail).union(link)


shell = build_shell()
base = build_base()
part = base.union(shell)
for yc, az in zip(K_Y, K_AXZ):
    part = part.union(build_knuckle(yc, az))
part = part.union(build_box())
part = part.union(build_thumb_roller())
part = part.union(build_brackets())

result = part
VIEW = {"azimuth": 45, "elevation": 26}
